import math
import cadquery as cq

# =====================================================================
# Bar clamp / hook bracket
#   Side profile lies in the YZ plane and is extruded along X (width).
#   Origin = centre of the large arch (axis of the clamped bar).
#   Four radial tapped holes on the flat top faces point at the bar axis;
#   a central slot hollows the body between two side walls.
# =====================================================================

# ---------------- main dimensions ----------------
W = 30.0             # body width (X)
RF = 49.25           # distance of the 4 flat top faces from the arch centre
FACE_STEP = 32.5     # angular pitch of the flat faces (deg from vertical)
R_ARCH = 16.8        # arch (bar seat) radius

# central slot between the side walls
SLOT_W = 15.0        # slot width (X)
WEB_T = 3.5          # web thickness left under the flat faces
SLOT_Y0 = -43.0      # slot start under the beak
SLOT_Y1 = 44.0       # slot end wall at the hook end

# radial tapped holes (threads modelled as a plain bore)
HOLE_D = 18.0
HOLE_DEPTH = 19.0
CB_D = 20.0          # counterbore
CB_DEPTH = 2.6

# hook end: outer arc centre (radius follows from tangency with the steep face)
CO = (6.5, -11.0)
FOOT_ANG = -26.5     # polar angle (deg) of the foot's outer corner on that arc

# beak / hook key points (Y, Z)
A = (-59.45, 36.35)  # beak tip, top edge
M = (-63.7, 24.75)   # beak tip, bottom edge
BEAK_ANG = 19.9      # beak underside slope (falls towards +Y)
H = (39.15, -28.3)   # foot bottom, inner corner
I = (44.95, -14.3)   # top of the foot inner face
J_Z = -3.9           # bottom of the short vertical wall right of the arch

TIP_FILLET = 6.0     # rounding of the beak tip corners

# beak tip pocket and holes
TIP_POCKET_W, TIP_POCKET_H, TIP_POCKET_D = 11.6, 4.8, 13.0
TIP_POCKET_OFF = -0.7        # pocket centre offset along the tip face
UH_D, UH_S, UH_DEPTH = 7.0, 7.2, 5.0   # underside hole: dia, pos. from tip, depth
PIN_D, PIN_DEPTH = 2.6, 11.0

# keyhole slot through the +X wall
KEY_ANG = 17.6       # deg above horizontal
KEY_LEN = 22.6       # arch centre -> centre of round end
KEY_R = 5.3

# small rectangular recesses on the +X face
SQ_ANG = 40.6        # deg from vertical
SQ_R = (20.75, 28.8)
SQ_A, SQ_B, SQ_DEPTH = 2.65, 4.3, 4.0

# notch in the foot inner face
NOTCH_W = 24.0
NOTCH_Z0 = -23.6
NOTCH_D = 8.0


# ---------------- helpers ----------------
def ang_pt(r, deg):
    a = math.radians(deg)
    return (r * math.sin(a), r * math.cos(a))


def corner(r, a1, a2):
    """Corner of two faces tangent to circle r at polar angles a1, a2 (deg)."""
    am = 0.5 * (a1 + a2)
    return ang_pt(r / math.cos(math.radians(0.5 * (a2 - a1))), am)


def on_face_line(r, deg, y):
    """Z on the face tangent to circle r at polar angle deg, for given Y."""
    s, c = math.sin(math.radians(deg)), math.cos(math.radians(deg))
    return (r - y * s) / c


def unit(v):
    n = math.hypot(*v)
    return (v[0] / n, v[1] / n)


def yz_plane(origin, normal):
    return cq.Plane(origin=cq.Vector(0, origin[0], origin[1]),
                    xDir=cq.Vector(1, 0, 0), normal=cq.Vector(0, normal[0], normal[1]))


# ---------------- profile points ----------------
C = corner(RF, -FACE_STEP, 0.0)
D = corner(RF, 0.0, FACE_STEP)
E = corner(RF, FACE_STEP, 2 * FACE_STEP)

# beak top runs from the tip A to the left slope face
_l_s, _l_c = math.sin(math.radians(FACE_STEP)), math.cos(math.radians(FACE_STEP))
_bt = unit((20.6, -2.85))
_t = (RF + A[0] * _l_s - A[1] * _l_c) / (-_bt[0] * _l_s + _bt[1] * _l_c)
B = (A[0] + _t * _bt[0], A[1] + _t * _bt[1])

# steep face tangent to the outer arc
n_st = ang_pt(1.0, 2 * FACE_STEP)
RO = RF - (CO[0] * n_st[0] + CO[1] * n_st[1])
F = (CO[0] + RO * n_st[0], CO[1] + RO * n_st[1])
_ag = math.radians(FOOT_ANG)
G = (CO[0] + RO * math.cos(_ag), CO[1] + RO * math.sin(_ag))
_ap = 0.5 * (math.atan2(F[1] - CO[1], F[0] - CO[0]) + _ag)
P = (CO[0] + RO * math.cos(_ap), CO[1] + RO * math.sin(_ap))

# arch: left end where the beak underside meets the arch circle
_bd = (math.cos(math.radians(BEAK_ANG)), -math.sin(math.radians(BEAK_ANG)))
_b = 2 * (M[0] * _bd[0] + M[1] * _bd[1])
_c = M[0] ** 2 + M[1] ** 2 - R_ARCH ** 2
_t = (-_b - math.sqrt(_b * _b - 4 * _c)) / 2
L = (M[0] + _t * _bd[0], M[1] + _t * _bd[1])
_la = math.atan2(L[1], L[0])
ARCH_MID = (R_ARCH * math.cos(0.5 * _la), R_ARCH * math.sin(0.5 * _la))
K = (R_ARCH, 0.0)
J = (R_ARCH, J_Z)

# ---------------- body ----------------
profile = (
    cq.Workplane("YZ")
    .moveTo(*A)
    .lineTo(*B)
    .lineTo(*C)
    .lineTo(*D)
    .lineTo(*E)
    .lineTo(*F)
    .threePointArc(P, G)
    .lineTo(*H)
    .lineTo(*I)
    .lineTo(*J)
    .lineTo(*K)
    .threePointArc(ARCH_MID, L)
    .lineTo(*M)
    .close()
)
body = profile.extrude(W / 2, both=True)

# rounded corners of the beak tip
body = (body.edges(cq.selectors.BoxSelector((-20, -66, 23), (20, -58, 38)))
        .edges("not |X").fillet(TIP_FILLET))

# ---------------- central slot ----------------
RC = RF - WEB_T
c1 = corner(RC, -FACE_STEP, 0.0)
c2 = corner(RC, 0.0, FACE_STEP)
c3 = corner(RC, FACE_STEP, 2 * FACE_STEP)
zl = on_face_line(RC, -FACE_STEP, SLOT_Y0)
zr = on_face_line(RC, 2 * FACE_STEP, SLOT_Y1)
_slope = (I[1] - J[1]) / (I[0] - J[0])
z_end_bot = J[1] + _slope * (SLOT_Y1 - J[0]) - 1.0
slot = (
    cq.Workplane("YZ")
    .moveTo(SLOT_Y0, -60)
    .lineTo(SLOT_Y0, zl)
    .lineTo(*c1)
    .lineTo(*c2)
    .lineTo(*c3)
    .lineTo(SLOT_Y1, zr)
    .lineTo(SLOT_Y1, z_end_bot)
    .lineTo(J[0] - 1.0, J[1] - 1.0)
    .lineTo(J[0] - 1.0, -60)
    .close()
    .extrude(SLOT_W / 2, both=True)
)
body = body.cut(slot)

# ---------------- radial tapped holes (4x) ----------------
for a in (-FACE_STEP, 0.0, FACE_STEP, 2 * FACE_STEP):
    n = ang_pt(1.0, a)
    pl = yz_plane((RF * n[0], RF * n[1]), (-n[0], -n[1]))
    body = body.cut(cq.Workplane(pl).circle(HOLE_D / 2).extrude(HOLE_DEPTH))
    body = body.cut(cq.Workplane(pl).circle(CB_D / 2).extrude(CB_DEPTH))

# ---------------- beak tip pocket ----------------
tu = unit((A[0] - M[0], A[1] - M[1]))      # up along the tip face
tn = (tu[1], -tu[0])                        # into the beak
tip_c = (0.5 * (A[0] + M[0]) + TIP_POCKET_OFF * tu[0],
         0.5 * (A[1] + M[1]) + TIP_POCKET_OFF * tu[1])
body = body.cut(cq.Workplane(yz_plane(tip_c, tn))
                .rect(TIP_POCKET_W, TIP_POCKET_H).extrude(TIP_POCKET_D))

# hole in the beak underside (into the pocket) and pin hole above it
uu = unit((L[0] - M[0], L[1] - M[1]))
un = (-uu[1], uu[0])
uh_pl = yz_plane((M[0] + UH_S * uu[0], M[1] + UH_S * uu[1]), un)
body = body.cut(cq.Workplane(uh_pl).circle(UH_D / 2).extrude(UH_DEPTH))
body = body.cut(cq.Workplane(uh_pl).circle(PIN_D / 2).extrude(PIN_DEPTH))

# ---------------- keyhole slot through the +X wall ----------------
ka = math.radians(KEY_ANG)
key_pl = cq.Plane(origin=cq.Vector(W / 2, 0, 0),
                  xDir=cq.Vector(0, math.cos(ka), math.sin(ka)),
                  normal=cq.Vector(-1, 0, 0))
body = body.cut(cq.Workplane(key_pl).center(KEY_LEN / 2, 0)
                .slot2D(KEY_LEN + 2 * KEY_R, 2 * KEY_R, 0)
                .extrude((W - SLOT_W) / 2 + 0.5))

# ---------------- two small rectangular recesses on the +X face ----------------
sa = math.radians(SQ_ANG)
for r in SQ_R:
    pl = cq.Plane(origin=cq.Vector(W / 2, r * math.sin(sa), r * math.cos(sa)),
                  xDir=cq.Vector(0, math.sin(sa), math.cos(sa)), normal=cq.Vector(-1, 0, 0))
    body = body.cut(cq.Workplane(pl).rect(SQ_A, SQ_B).extrude(SQ_DEPTH))

# ---------------- notch in the foot inner face ----------------
fu = unit((I[0] - H[0], I[1] - H[1]))      # up along the foot face
fn = (fu[1], -fu[0])                        # into the foot
f_len = math.hypot(I[0] - H[0], I[1] - H[1])
s0 = (NOTCH_Z0 - H[1]) / fu[1]
s1 = f_len + 0.01
sm = 0.5 * (s0 + s1)
body = body.cut(cq.Workplane(yz_plane((H[0] + sm * fu[0], H[1] + sm * fu[1]), fn))
                .rect(NOTCH_W, s1 - s0).extrude(NOTCH_D))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
